"""Cross-shaped mounting plate with four raised corner bosses.

Flat plate (XY, underside at z=0) with a pinched central body: straight
sides blending into the arms, concave waists top and bottom.  Four arms run
out to cylindrical bosses that stand proud of the plate, blended into the arm
tops with a concave fillet.  Through holes in the bosses and two small holes
on the X axis.
"""
import math
import cadquery as cq

# ---------------- driving dimensions (mm) ----------------
# boss centres (x, y) - the part is not perfectly symmetric
BOSS_TR = (53.65, 43.72)
BOSS_TL = (-53.55, 43.48)
BOSS_BL = (-54.74, -44.12)
BOSS_BR = (53.70, -44.12)
BOSS_D = 8.9          # boss outer diameter
ARM_W = 8.7           # arm width (slightly narrower than the boss)
BOSS_H = 6.0          # boss height from underside
HOLE_D = 3.7          # boss through-hole
PLATE_T = 3.65        # plate thickness
# the arm edges run from kinks on the body outline to tangency with a circle
# of ARM_W/2 around the boss centre.  Kinks: |y| on the side flare and |x|
# on the waist, per quadrant
KINK_SIDE_Y = {"TR": 29.0, "TL": 29.2, "BL": 28.8, "BR": 29.2}
KINK_WAIST_X = {"TR": 29.4, "TL": 27.4, "BL": 27.5, "BR": 29.35}

# central body: straight sides x = +-SIDE_W, flaring out towards the arms
# beyond |y| > y0 as  x = W + c*(sqrt(1+((|y|-y0)/d)^2)-1)   (per quadrant)
SIDE_W = 37.40
SIDE = {              # quadrant: (y0, c, d)
    "TR": (17.9, 5.584, 6.0),
    "BR": (13.2, 9.332, 11.6),
    "TL": (12.4, 62.6, 40.0),
    "BL": (10.5, 51.5, 40.0),
}
# waists: |y| = H + a*(sqrt(1+((x-xc)/b)^2)-1)   (top / bottom)
WAIST = {             # half: (H, a, b, xc)
    "T": (17.23, 7.620, 12.1, 0.45),
    "B": (16.47, 5.633, 9.2, -0.30),
}

SMALL_X = 30.26       # two small holes on the X axis
SMALL_D = 3.35

BOSS_FILLET = 1.5     # concave blend boss -> arm top

VIEW = {"azimuth": 45, "elevation": 26}

rb = BOSS_D / 2.0
ra = ARM_W / 2.0


# ---------------- outline curves ----------------
def side_x(q, y):
    """|x| of the side flare of quadrant q at height y"""
    y0, c, d = SIDE[q]
    t = max(abs(y) - y0, 0.0)
    return SIDE_W + c * (math.sqrt(1.0 + (t / d) ** 2) - 1.0)


def side_slope(q, y):
    """d|x|/d|y|"""
    y0, c, d = SIDE[q]
    t = max(abs(y) - y0, 0.0)
    return c * t / (d ** 2 * math.sqrt(1.0 + (t / d) ** 2))


def waist_y(h, x):
    """|y| of the waist h ('T' or 'B') at x"""
    H, a, b, xc = WAIST[h]
    return H + a * (math.sqrt(1.0 + ((x - xc) / b) ** 2) - 1.0)


def waist_slope(h, x):
    """d|y|/dx"""
    H, a, b, xc = WAIST[h]
    u = (x - xc) / b
    return a * u / (b * math.sqrt(1.0 + u * u))


def tangent_point(K, C, r, cw):
    """tangent point on circle (C, r) of the line from K (first-quadrant
    form); cw picks the tangent clockwise of K->C"""
    vx, vy = C[0] - K[0], C[1] - K[1]
    d = math.hypot(vx, vy)
    phi = math.atan2(vy, vx) + (-1 if cw else 1) * math.asin(r / d)
    L = math.sqrt(d * d - r * r)
    return (K[0] + L * math.cos(phi), K[1] + L * math.sin(phi))


def arm(q, boss):
    """Arm of quadrant q.  Returns the edge points at the boss (T1 side edge,
    T2 waist edge - tangency points on the ARM_W/2 circle, inside the boss),
    the kinks on the body outline (Ks side flare, Kw waist) and the inward
    unit directions of both edges."""
    sx = 1.0 if boss[0] > 0 else -1.0
    sy = 1.0 if boss[1] > 0 else -1.0
    h = "T" if sy > 0 else "B"
    C = (abs(boss[0]), abs(boss[1]))
    ys = KINK_SIDE_Y[q]
    Ks = (side_x(q, ys), ys)
    xw = KINK_WAIST_X[q]
    Kw = (xw, waist_y(h, sx * xw))
    T1 = tangent_point(Ks, C, ra, True)
    T2 = tangent_point(Kw, C, ra, False)

    def unit(a, b):
        L = math.hypot(b[0] - a[0], b[1] - a[1])
        return ((b[0] - a[0]) / L, (b[1] - a[1]) / L)

    m = lambda p: (sx * p[0], sy * p[1])
    return {"T1": m(T1), "T2": m(T2), "Ks": m(Ks), "Kw": m(Kw),
            "d1": m(unit(T1, Ks)), "d2": m(unit(T2, Kw)), "c": boss,
            "sx": sx, "sy": sy}


quad = {
    "TR": arm("TR", BOSS_TR),
    "TL": arm("TL", BOSS_TL),
    "BL": arm("BL", BOSS_BL),
    "BR": arm("BR", BOSS_BR),
}


def flare(wp, q, outward, n=4):
    """spline along the side flare of quadrant q, between the end of the
    straight side and the kink (outward = travelling towards the kink)"""
    sx, sy = quad[q]["sx"], quad[q]["sy"]
    y0 = SIDE[q][0]
    yk = abs(quad[q]["Ks"][1])
    ys = [y0 + (yk - y0) * i / n for i in range(n + 1)]
    if not outward:
        ys = ys[::-1]
    pts = [(sx * side_x(q, y), sy * y) for y in ys]
    pts[0 if not outward else -1] = quad[q]["Ks"]
    sgn = 1.0 if outward else -1.0
    t0 = (sgn * sx * side_slope(q, ys[0]), sgn * sy)
    t1 = (sgn * sx * side_slope(q, ys[-1]), sgn * sy)
    return wp.spline(pts[1:], tangents=[t0, t1], includeCurrent=True)


def waist(wp, h, xa, xb, end, n=8):
    """spline along waist h from x=xa (current point) to the kink `end`"""
    sy = 1.0 if h == "T" else -1.0
    xs = [xa + (xb - xa) * i / n for i in range(n + 1)]
    pts = [(x, sy * waist_y(h, x)) for x in xs]
    pts[-1] = end
    sgn = 1.0 if xb > xa else -1.0
    t0 = (sgn, sgn * sy * waist_slope(h, xa))
    t1 = (sgn, sgn * sy * waist_slope(h, xb))
    return wp.spline(pts[1:], tangents=[t0, t1], includeCurrent=True)


def outline(height):
    q = quad
    wp = cq.Workplane("XY").moveTo(SIDE_W, -SIDE["BR"][0]).lineTo(SIDE_W, SIDE["TR"][0])
    wp = flare(wp, "TR", True)
    wp = wp.lineTo(*q["TR"]["T1"]).lineTo(*q["TR"]["T2"]).lineTo(*q["TR"]["Kw"])
    wp = waist(wp, "T", q["TR"]["Kw"][0], q["TL"]["Kw"][0], q["TL"]["Kw"])
    wp = wp.lineTo(*q["TL"]["T2"]).lineTo(*q["TL"]["T1"]).lineTo(*q["TL"]["Ks"])
    wp = flare(wp, "TL", False)
    wp = wp.lineTo(-SIDE_W, -SIDE["BL"][0])
    wp = flare(wp, "BL", True)
    wp = wp.lineTo(*q["BL"]["T1"]).lineTo(*q["BL"]["T2"]).lineTo(*q["BL"]["Kw"])
    wp = waist(wp, "B", q["BL"]["Kw"][0], q["BR"]["Kw"][0], q["BR"]["Kw"])
    wp = wp.lineTo(*q["BR"]["T2"]).lineTo(*q["BR"]["T1"]).lineTo(*q["BR"]["Ks"])
    wp = flare(wp, "BR", False)
    wp = wp.close()
    return wp.extrude(height)


plate = outline(PLATE_T)

boss_pts = [quad[k]["c"] for k in ("TR", "TL", "BL", "BR")]
bosses = cq.Workplane("XY").pushPoints(boss_pts).circle(rb).extrude(BOSS_H)
body = plate.union(bosses)

# concave blend between each boss and the top of its arm: a revolved fillet
# ring clipped to the arm strip on the inner side of the boss
f = BOSS_FILLET
c45 = math.cos(math.radians(45))
ring = (
    cq.Workplane("XZ")
    .moveTo(rb - 0.6, PLATE_T)
    .lineTo(rb + f, PLATE_T)
    .threePointArc((rb + f - f * c45, PLATE_T + f - f * c45), (rb, PLATE_T + f))
    .lineTo(rb - 0.6, PLATE_T + f)
    .close()
    .revolve(360, (0, 0, 0), (0, 1, 0))
)
L_clip = rb + f + 2.0
for k in ("TR", "TL", "BL", "BR"):
    qd = quad[k]
    cx, cy = qd["c"]
    d1, d2 = qd["d1"], qd["d2"]
    out_ang = math.degrees(math.atan2(-(d1[1] + d2[1]), -(d1[0] + d2[0])))
    a, b = qd["T1"], qd["T2"]
    strip = (
        cq.Workplane("XY").workplane(offset=PLATE_T - 0.5)
        .polyline([a, b,
                   (b[0] + L_clip * d2[0], b[1] + L_clip * d2[1]),
                   (a[0] + L_clip * d1[0], a[1] + L_clip * d1[1])])
        .close()
        .extrude(f + 1.0)
    )
    blend = (
        ring.rotate((0, 0, 0), (0, 0, 1), out_ang)
        .translate((cx, cy, 0))
        .intersect(strip)
    )
    body = body.union(blend)
body = body.clean()

# through holes
cutters = (
    cq.Workplane("XY").workplane(offset=-1.0)
    .pushPoints(boss_pts).circle(HOLE_D / 2).extrude(BOSS_H + 2.0)
)
cutters = cutters.union(
    cq.Workplane("XY").workplane(offset=-1.0)
    .pushPoints([(SMALL_X, 0), (-SMALL_X, 0)]).circle(SMALL_D / 2)
    .extrude(PLATE_T + 2.0)
)
body = body.cut(cutters)

result = body
